import cadquery as cq

# =====================================================================
#  V-groove pulley with a servo-horn pocket, two pan-head screws with
#  washers, a hub boss underneath and the screw tips poking out below.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
D = 65.0                 # pulley outer diameter
R = D / 2.0
T = 8.4                  # pulley body thickness (bottom face at z=0)
FLANGE_BOT = 2.45        # cylindrical land below the groove
GROOVE_W = 3.5           # V-groove width at the rim
GROOVE_DEPTH = 1.75      # V-groove depth (90 deg V)

POCKET_R = 12.6          # main round pocket radius at the rim (servo horn seat)
POCKET_R_FLOOR = 12.3    # radius at the floor (drafted wall)
POCKET_DEPTH = 3.6
SCREW_OFF = 8.9          # screw positions (0, +/-SCREW_OFF)
LOBE_OFF = 8.6           # lobe centre offset along +/-Y
LOBE_R = 5.7             # lobe radius
LOBE_EXTRA_DEPTH = 0.1   # lobe floors are spot-faced slightly deeper

HOLE_D = 2.0             # small horn holes in the pocket floor
HOLE_DEPTH = 1.5
HOLE_X = 8.9             # column of three holes at x = +/-HOLE_X
HOLE_Y = 4.3             # pitch of the three holes
SIDE_HOLE_X = 4.3        # holes beside the screws (partly under washers)

HUB_GROOVE_RO = 5.15     # annular groove around the central ring
HUB_GROOVE_RI = 4.05
HUB_GROOVE_DEPTH = 1.2
HUB_BORE_D = 6.9         # shallow counterbore inside the ring
HUB_BORE_DEPTH = 0.8
HUB_HOLE_D = 3.6         # through hole

BOSS_D = 10.3            # boss under the pulley
BOSS_H = 2.6
BOSS_BORE_D = 6.5        # spline bore from below
BOSS_BORE_DEPTH = 4.6    # measured from the boss bottom face
BOSS_CHAMFER = 0.12
BOSS_SPOT_R = 5.75       # shallow spot-face ring around the boss root
BOSS_SPOT_DEPTH = 0.1

PIN_D = 3.0              # screw tips protruding below
PIN_H = 1.9
PIN_CHAMFER = 0.15

WASHER_D = 8.0
WASHER_T = 0.55
HEAD_D = 5.3             # pan head
HEAD_H = 1.7
HEAD_FLANK_R = 0.90      # dome profile control points (fractions of radius / height)
HEAD_FLANK_Z = 0.62
HEAD_CROWN_R = 0.58
HEAD_CROWN_Z = 0.93
RECESS_W = 1.1           # Phillips recess arm width at the centre
RECESS_TIP_W = 0.6       # arm width at the tips
RECESS_L = 3.4           # Phillips recess span
RECESS_DEPTH = 0.9
RECESS_CONE_R = 1.9      # recess cone radius at the crown height
RECESS_TAPER = 12.0      # deg, sloped arm flanks of the cross recess

floor_z = T - POCKET_DEPTH

# seams of revolved / cylindrical convex faces are turned to the back
CONVEX_SEAM_ROT = 180.0
DOME_SEAM_ROT = 135.0


def zcyl(r, h, z0=0.0, rot=CONVEX_SEAM_ROT):
    """Convex cylinder on the Z axis with its seam rotated away."""
    c = cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(h)
    return c.rotate((0, 0, 0), (0, 0, 1), rot)


# ---------------- pulley body (revolved profile) ----------------
g_bot = FLANGE_BOT
g_top = FLANGE_BOT + GROOVE_W
g_mid = (g_bot + g_top) / 2.0
profile = [
    (0.0, 0.0),
    (R, 0.0),
    (R, g_bot),
    (R - GROOVE_DEPTH, g_mid),
    (R, g_top),
    (R, T),
    (0.0, T),
]
body = (
    cq.Workplane("XZ")
    .polyline(profile)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), CONVEX_SEAM_ROT)
)

# ---------------- boss under the pulley ----------------
boss = (
    zcyl(BOSS_D / 2, BOSS_H + 0.5, -BOSS_H)
    .faces("<Z").edges().chamfer(BOSS_CHAMFER)
)
body = body.union(boss)
spot_ring = (
    cq.Workplane("XY").workplane(offset=-0.5)
    .circle(BOSS_SPOT_R).circle(BOSS_D / 2).extrude(0.5 + BOSS_SPOT_DEPTH)
)
body = body.cut(spot_ring)

# ---------------- screw tips below ----------------
for s in (1, -1):
    pin = (
        zcyl(PIN_D / 2, PIN_H + 0.5, -PIN_H)
        .faces("<Z").edges().chamfer(PIN_CHAMFER)
        .translate((0, s * SCREW_OFF, 0))
    )
    body = body.union(pin)

# ---------------- top pocket: drafted round seat + two washer lobes ----------------
# main seat: slight draft (floor radius < rim radius)
pocket_slope = (POCKET_R - POCKET_R_FLOOR) / POCKET_DEPTH
pocket = cq.Workplane("XY").add(
    cq.Solid.makeCone(
        POCKET_R_FLOOR, POCKET_R + pocket_slope * 1.0,
        POCKET_DEPTH + 1.0,
        cq.Vector(0, 0, floor_z), cq.Vector(0, 0, 1),
    )
)
# lobes: round clearance pockets for the washers, spot-faced a hair below
# the floor outside the main seat
for s in (1, -1):
    lobe = (
        cq.Workplane("XY").workplane(offset=floor_z)
        .center(0, s * LOBE_OFF).circle(LOBE_R).extrude(POCKET_DEPTH + 1)
    )
    pocket = pocket.union(lobe)
body = body.cut(pocket)
for s in (1, -1):
    spot = (
        cq.Workplane("XY").workplane(offset=floor_z - LOBE_EXTRA_DEPTH)
        .center(0, s * LOBE_OFF).circle(LOBE_R).extrude(LOBE_EXTRA_DEPTH + 0.01)
        .cut(
            cq.Workplane("XY").workplane(offset=floor_z - 1)
            .circle(POCKET_R_FLOOR).extrude(2)
        )
    )
    body = body.cut(spot)

# small blind holes in the pocket floor
hole_pts = [(sx * HOLE_X, y) for sx in (1, -1) for y in (-HOLE_Y, 0.0, HOLE_Y)]
hole_pts += [(sx * SIDE_HOLE_X, sy * SCREW_OFF) for sx in (1, -1) for sy in (1, -1)]
holes = (
    cq.Workplane("XY").workplane(offset=floor_z - HOLE_DEPTH)
    .pushPoints(hole_pts).circle(HOLE_D / 2).extrude(HOLE_DEPTH + 0.5)
)
body = body.cut(holes)

# ---------------- central hub features ----------------
groove = (
    cq.Workplane("XY").workplane(offset=floor_z - HUB_GROOVE_DEPTH)
    .circle(HUB_GROOVE_RO).extrude(HUB_GROOVE_DEPTH + 0.5)
    .cut(zcyl(HUB_GROOVE_RI, HUB_GROOVE_DEPTH + 1.0, floor_z - HUB_GROOVE_DEPTH - 0.25))
)
body = body.cut(groove)
bore = (
    cq.Workplane("XY").workplane(offset=floor_z - HUB_BORE_DEPTH)
    .circle(HUB_BORE_D / 2).extrude(HUB_BORE_DEPTH + 0.5)
)
body = body.cut(bore)
thru = (
    cq.Workplane("XY").workplane(offset=-BOSS_H - 1)
    .circle(HUB_HOLE_D / 2).extrude(T + BOSS_H + 2)
)
body = body.cut(thru)
bot_bore = (
    cq.Workplane("XY").workplane(offset=-BOSS_H - 1)
    .circle(BOSS_BORE_D / 2).extrude(BOSS_BORE_DEPTH + 1)
)
body = body.cut(bot_bore)


# ---------------- washers + pan head screws in the lobes ----------------
def pan_head():
    """Domed pan head with a Phillips cross recess (cross prism limited by
    an inverted cone, so the arms run out towards the rim)."""
    a = HEAD_D / 2.0
    h = HEAD_H
    # full, flattened dome: steep flank rolling over into a broad crown
    crown = [
        (a, 0.0),
        (a * HEAD_FLANK_R, h * HEAD_FLANK_Z),
        (a * HEAD_CROWN_R, h * HEAD_CROWN_Z),
        (0.0, h),
    ]
    head = (
        cq.Workplane("XZ")
        .moveTo(0, 0)
        .lineTo(a, 0)
        .spline(crown[1:], tangents=[(0, 1), (-1, 0)], includeCurrent=True)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), DOME_SEAM_ROT)
    )
    # four-pointed cross outline (arms narrowing towards their tips)
    w = RECESS_W / 2.0
    L = RECESS_L / 2.0
    tip = RECESS_TIP_W / 2.0
    cross = [
        (L, tip), (w, w), (tip, L), (-tip, L), (-w, w), (-L, tip),
        (-L, -tip), (-w, -w), (-tip, -L), (tip, -L), (w, -w), (L, -tip),
    ]
    z_bot = h - RECESS_DEPTH
    z_top = h + 0.05
    prism = (
        cq.Workplane(cq.Plane(origin=(0, 0, z_top), xDir=(1, 0, 0),
                              normal=(0, 0, -1)))
        .polyline(cross).close()
        .extrude(z_top - z_bot, taper=RECESS_TAPER)
    )
    cone_top = RECESS_CONE_R * (RECESS_DEPTH + 0.5) / RECESS_DEPTH
    cone = cq.Workplane("XY").add(
        cq.Solid.makeCone(
            0.0, cone_top, RECESS_DEPTH + 0.5,
            cq.Vector(0, 0, z_bot), cq.Vector(0, 0, 1),
        )
    ).rotate((0, 0, 0), (0, 0, 1), 45)   # cone seam between the arms
    cutter = prism.intersect(cone)
    return head.cut(cutter)


head_proto = pan_head()
for s in (1, -1):
    seat_z = floor_z
    washer = zcyl(WASHER_D / 2, WASHER_T, seat_z).translate((0, s * SCREW_OFF, 0))
    body = body.union(washer)
    body = body.union(head_proto.translate((0, s * SCREW_OFF, seat_z + WASHER_T)))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
